"""Rounded-square block with a round opening in the top face that leads into a
wider, hidden cylindrical cavity (an undercut pocket held by a thin top lip).

Read from the reference views:
  * plan: 60 x 60 square, R15 vertical corner rounds, thickness 16
  * top: centred round opening, ~0.85 deep lip (its wall shows as the first
    bright band inside the hole)
  * below the lip a much wider, flat-bottomed cavity; its far wall is the second
    bright band seen through the opening, whose flat lower rim shows the cavity
    is about twice the opening diameter
  * bottom face and sides plain, all edges sharp
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0             # side length of the square block (plan view)
T = 16.0             # block thickness
R_CORNER = 15.0      # vertical corner radius (plan view)

D_OPEN = 16.0        # diameter of the round opening in the top face
T_LIP = 0.85         # thickness of the top lip around the opening
D_CAVITY = 30.0      # diameter of the hidden cavity under the lip
H_CAVITY = 4.5       # height of the hidden cavity

# cylinder seams are placed on the +-45 deg diagonal, where the inside walls
# are never seen through the opening
SEAM_DIR = (-1, -1, 0)

# ---------------- block: rounded-square plate ----------------
block = (
    cq.Workplane("XY")
    .rect(W, W)
    .extrude(T)
    .edges("|Z")
    .fillet(R_CORNER)
)

z_lip = T - T_LIP            # underside of the lip = roof of the cavity


def disc(diameter, z0, height):
    """Vertical cylinder (tool body) centred on the block axis."""
    plane = cq.Plane(origin=(0, 0, z0), xDir=SEAM_DIR, normal=(0, 0, 1))
    return cq.Workplane(plane).circle(diameter / 2.0).extrude(height)


# round opening through the lip (tool overshoots above and below)
opening = disc(D_OPEN, z_lip - 0.5, T_LIP + 1.0)

# wider cylindrical cavity directly under the lip
cavity = disc(D_CAVITY, z_lip - H_CAVITY, H_CAVITY)

result = block.cut(opening).cut(cavity)

VIEW = {"azimuth": 45, "elevation": 26}
